import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 211.0            # overall length (disc front face -> flange back face)
D_FLANGE = 100.0     # trumpet flange diameter
D_DISC = 80.0        # small end disc diameter
T_DISC = 6.4         # small end disc thickness
D_SHAFT = 30.0       # shaft diameter
R_FLARE = 42.5       # radius of the concave flare arc
FLARE_LEN = 45.0     # axial distance from flange back face to where the flare leaves the shaft
FIL_DISC_BACK = 3.8  # fillet on disc back outer edge
FIL_DISC_SHAFT = 5.5 # fillet between disc and shaft
FIL_RIM = 2.0        # fillet where flare meets flange rim

SLOT_W = 5.0         # slot width
SLOT_R_IN = 16.6     # slot inner end radius (from axis)
SLOT_R_OUT = 35.5    # slot outer end radius
N_SLOTS = 4
SEAM_ROT = 145.0     # rotation of the revolved body about its axis (seam placement)

r_f = D_FLANGE / 2.0
r_d = D_DISC / 2.0
r_s = D_SHAFT / 2.0

# flare arc: tangent to shaft, centre at (r_s + R_FLARE, y_start)
y_start = L - FLARE_LEN
cx, cy = r_s + R_FLARE, y_start
dy_end = math.sqrt(R_FLARE ** 2 - (cx - r_f) ** 2)
y_rim = y_start + dy_end          # where the arc meets the rim cylinder
# mid point on arc
ang_end = math.atan2(dy_end, r_f - cx)    # angle of end point about centre
ang_start = math.pi                        # start point at (r_s, y_start)
ang_mid = 0.5 * (ang_start + ang_end)
mid = (cx + R_FLARE * math.cos(ang_mid), cy + R_FLARE * math.sin(ang_mid))

# ---------------- revolved body (axis = Y) ----------------
prof = (
    cq.Workplane("XY")
    .moveTo(0, 0)
    .lineTo(r_d, 0)
    .lineTo(r_d, T_DISC)
    .lineTo(r_s, T_DISC)
    .lineTo(r_s, y_start)
    .threePointArc(mid, (r_f, y_rim))
    .lineTo(r_f, L)
    .lineTo(0, L)
    .close()
)
body = prof.revolve(360, (0, 0, 0), (0, 1, 0))


def circ_edge_sel(radius, y, tol=0.05):
    def f(objs):
        out = []
        for e in objs:
            if e.geomType() != "CIRCLE":
                continue
            c = e.Center()
            if abs(e.radius() - radius) < tol and abs(c.y - y) < tol:
                out.append(e)
        return out
    return f


class _Sel(cq.Selector):
    def __init__(self, fn):
        self.fn = fn

    def filter(self, objectList):
        return self.fn(objectList)


body = body.edges(_Sel(circ_edge_sel(r_d, T_DISC))).fillet(FIL_DISC_BACK)
body = body.edges(_Sel(circ_edge_sel(r_s, T_DISC))).fillet(FIL_DISC_SHAFT)
body = body.edges(_Sel(circ_edge_sel(r_f, y_rim))).fillet(FIL_RIM)
# turn the revolve seam to the underside (purely cosmetic)
body = body.rotate((0, 0, 0), (0, 1, 0), SEAM_ROT)

# ---------------- radial through-slots in the small disc ----------------
slot_len = SLOT_R_OUT - SLOT_R_IN
slot_mid = 0.5 * (SLOT_R_IN + SLOT_R_OUT)
cut_depth = T_DISC + FIL_DISC_SHAFT + 2.0

slots = None
for i in range(N_SLOTS):
    a = 360.0 / N_SLOTS * i
    s = (
        cq.Workplane("XZ", origin=(0, -1.0, 0))
        .center(slot_mid * math.cos(math.radians(a)), slot_mid * math.sin(math.radians(a)))
        .slot2D(slot_len, SLOT_W, angle=a)
        .extrude(-(cut_depth + 1.0))
    )
    slots = s if slots is None else slots.union(s)

result = body.cut(slots)

VIEW = {"azimuth": 45, "elevation": 26}
